import cadquery as cq

# ---------------- driving dimensions (mm) ----------------
W = 180.0          # plate width  (X)
H = 100.0          # plate height (Z)
T = 3.2            # plate thickness at the outer margin (Y)
R_CORNER = 4.0     # plan corner radius of the plate
FRONT_FIL = 1.2    # rounding of the front outer edge

RIM_INSET = 2.2    # back rim offset from the outer edge
RIM_WALL = 1.8     # back rim wall thickness
RIM_H = 1.2        # back rim height above the outer margin
RIM_CHAMFER = 0.3  # small chamfer on the rim's outer top edge
POCKET_DEPTH = 1.0 # pocket floor sunk below the outer margin level

CORNER_HOLE_OFF = 5.5   # corner hole centre distance from edges
HOLE_D = 1.5            # through bore of the screw holes
CSK_D = 2.9             # countersink diameter on the front face
CSK_ANGLE = 90.0

PAD_OFF = 12.2     # circular pad seats distance from edges
PAD_D = 7.0
PAD_DEPTH = 0.3

BOSS_OD = 4.0      # screw bosses on the back (flush with rim top)
BOSS_BORE = 2.4    # bore in the bosses from the back
BOSS_BORE_Y = 1.0  # level (from the front face) where the boss bore stops
BOSS_PTS = [(0.0, 18.5), (-16.0, -20.3), (16.0, -20.3)]
CORNER_BOSS_D = 4.0  # small bosses around the corner holes, merged into the rim corners

TAB_X0 = 37.0      # locating tab on the back, joined to the bottom rim
TAB_X1 = 50.0
TAB_TOP = -31.0

VIEW = {"azimuth": 45, "elevation": 26}

# Plate lies in the XZ plane; front face at Y=0 (faces -Y), back toward +Y.
# Workplane("XZ") has normal -Y, so a negative extrude grows toward +Y.
Y_TOP = T + RIM_H            # back-most level (rim top, boss tops)
Y_FLOOR = T - POCKET_DEPTH   # pocket floor level


def wp_at(y):
    return cq.Workplane("XZ", origin=(0, y, 0))


def rrect(y, w, h, r, depth):
    return wp_at(y).sketch().rect(w, h).vertices().fillet(r).finalize().extrude(-depth)


# ---------------- main plate ----------------
plate = rrect(0.0, W, H, R_CORNER, T)
plate = plate.faces("<Y").edges().fillet(FRONT_FIL)

# ---------------- raised back block with rim ----------------
ow = W - 2 * RIM_INSET
oh = H - 2 * RIM_INSET
iw = ow - 2 * RIM_WALL
ih = oh - 2 * RIM_WALL
r_out = max(R_CORNER - RIM_INSET, 0.6)
r_in = max(r_out - RIM_WALL, 0.3)

block = rrect(T, ow, oh, r_out, RIM_H)
block = block.faces(">Y").edges().chamfer(RIM_CHAMFER)
part = plate.union(block)

# pocket inside the rim, sunk slightly below the margin level
pocket = rrect(Y_FLOOR, iw, ih, r_in, Y_TOP - Y_FLOOR + 1.0)
part = part.cut(pocket)

# ---------------- locating tab on the back ----------------
z_in_bot = -ih / 2.0
tab_len = TAB_TOP - z_in_bot + 0.3
tab = (
    wp_at(Y_FLOOR)
    .center((TAB_X0 + TAB_X1) / 2.0, z_in_bot - 0.3 + tab_len / 2.0)
    .rect(TAB_X1 - TAB_X0, tab_len)
    .extrude(-(Y_TOP - Y_FLOOR))
)
part = part.union(tab)

# ---------------- screw bosses on the back ----------------
bosses = wp_at(Y_FLOOR).pushPoints(BOSS_PTS).circle(BOSS_OD / 2.0).extrude(-(Y_TOP - Y_FLOOR))
part = part.union(bosses)

# ---------------- corner bosses (around the corner screw holes) ----------------
hx = W / 2 - CORNER_HOLE_OFF
hz = H / 2 - CORNER_HOLE_OFF
corner_pts = [(hx, hz), (-hx, hz), (hx, -hz), (-hx, -hz)]
cbosses = wp_at(Y_FLOOR).pushPoints(corner_pts).circle(CORNER_BOSS_D / 2.0).extrude(-(Y_TOP - Y_FLOOR))
part = part.union(cbosses)

# ---------------- countersunk holes from the front ----------------

# face workplane on the front: xDir=+X, yDir=+Z, drilling toward +Y
for pts in (corner_pts, BOSS_PTS):
    part = (
        part.faces("<Y").workplane(centerOption="ProjectedOrigin", origin=(0, 0, 0))
        .pushPoints(pts)
        .cskHole(HOLE_D, CSK_D, CSK_ANGLE)
    )

# larger bore in the back bosses
bores = wp_at(Y_TOP + 0.5).pushPoints(BOSS_PTS).circle(BOSS_BORE / 2.0).extrude(Y_TOP + 0.5 - BOSS_BORE_Y)
part = part.cut(bores)

# ---------------- shallow circular pad seats on the front ----------------
px = W / 2 - PAD_OFF
pz = H / 2 - PAD_OFF
pad_pts = [(px, pz), (-px, pz), (px, -pz), (-px, -pz)]
pads = wp_at(0.0).pushPoints(pad_pts).circle(PAD_D / 2.0).extrude(-PAD_DEPTH)
part = part.cut(pads)

result = part
